import math
import cadquery as cq

# =====================================================================
# Curved clevis link (rocker arm): banana-shaped side profile (Y-Z),
# clevis forks at both ends (slots through Y), the -X tines joggled out,
# two lightening windows through X, pin holes along X.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
PIN_Z = 100.0          # pins at Z = +PIN_Z (top) and -PIN_Z (bottom)
R_TOP = 15.0           # top end radius (Y-Z profile)
R_BOT = 23.5           # bottom end radius (Y-Z profile)
BOW_OUT = -30.5        # extreme -Y of the convex (front) edge
BOW_IN = 6.0           # extreme -Y of the concave (back) edge
PIN_D = 6.5            # pin hole diameter

X_MIN, X_MAX = -24.0, 24.0   # overall thickness
X_BODY = -10.0               # -X face of the middle body (joggled in)
TOP_GAP = (-11.5, 12.8)      # top clevis slot (X range)
TOP_SLOT_Z = 73.3            # top slot floor height at its front (Y = SLOT_Y_FRONT_T)
TOP_SLOT_TILT = -0.14        # floor square to the leaning upper arm: dZ/dY
SLOT_Y_FRONT_T = -21.0
TOP_SLOT_R = (3.5, 5.0)      # slot floor corner radii (X-Z), (-X, +X)
BOT_GAP = (-12.7, 12.4)      # bottom clevis slot
BOT_SLOT_Z = -80.6           # bottom slot roof height at its front (Y = SLOT_Y_FRONT_B)
BOT_SLOT_TILT = 0.13         # roof square to the leaning lower arm: dZ/dY
SLOT_Y_FRONT_B = -27.0
BOT_SLOT_R = (5.8, 5.8)
# rounding where the slot floor/roof meets the front (-Y) / back (+Y) faces
TOP_SLOT_EDGE_R = (4.0, 2.5)     # (front, back)
BOT_SLOT_EDGE_R = (2.0, 4.0)     # (front, back)
JOG_TOP = (73.0, 40.0)       # Z range of upper joggle (outer->body)
JOG_BOT = (-37.8, -63.8)     # Z range of lower joggle (body->outer), at back
JOG_BOT_SKEW = 0.13          # lower joggle tilts with the arm: dZ/dY
JOG_BOT_YREF = 14.0          # Y where the lower joggle sits at JOG_BOT

WIN_MARGIN = 9.3             # window inset from profile edges
# windows: flat inner end at z_in, slanted outer end through (y_ref, z_out)
WIN1 = dict(z_in=15.9, z_out=56.4, y_ref=-15.3, slope=-0.138)
WIN2 = dict(z_in=3.7, z_out=-39.5, y_ref=-21.1, slope=0.164)
WIN_R = 2.8

EDGE_R = 2.0                 # general edge rounding

# conical thrust pad around the top pin on the inner face of the +X tine
PAD_X = 8.1                  # pad face (X)
PAD_R = 15.6                 # pad face radius (just over R_TOP)
PAD_R_BASE = 19.6            # radius where it meets the tine inner face

# keyhole pocket on the outer face of the bottom -X tine
KEY_DEPTH = 6.0
KEY_CIRC = (-1.0, -0.5, 9.75)        # (dY, dZ, r) relative to bottom pin
KEY_SLOT = (-5.2, 8.6, 25.5)         # (dY centre, width, top dZ)

BIG = 80.0


# ---------------- side (Y-Z) banana profile ----------------
def tangent_arc(sign, extreme):
    """Arc tangent to both end circles. sign=-1: circles inside (convex edge),
    sign=+1: circles outside (concave edge). extreme = min Y of the arc."""
    def f(R):
        a = extreme + R
        rhs = (R + sign * R_TOP) ** 2 - (R + sign * R_BOT) ** 2
        b = -rhs / (4.0 * PIN_Z)
        return math.hypot(a, b - PIN_Z) - (R + sign * R_TOP), a, b

    lo, hi = 40.0, 20000.0
    flo = f(lo)[0]
    for _ in range(200):
        mid = 0.5 * (lo + hi)
        fm = f(mid)[0]
        if (fm > 0) == (flo > 0):
            lo, flo = mid, fm
        else:
            hi = mid
    R = 0.5 * (lo + hi)
    _, a, b = f(R)
    return a, b, R


def tpoint(c, R, p):
    dx, dy = p[0] - c[0], p[1] - c[1]
    d = math.hypot(dx, dy)
    return (c[0] + R * dx / d, c[1] + R * dy / d)


def arc_mid(c, R, p1, p2):
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    a2 = math.atan2(p2[1] - c[1], p2[0] - c[0])
    d = (a2 - a1 + math.pi) % (2.0 * math.pi) - math.pi
    am = a1 + 0.5 * d
    return (c[0] + R * math.cos(am), c[1] + R * math.sin(am))


aL, bL, RL = tangent_arc(-1, BOW_OUT)   # convex (-Y) edge
aR, bR, RR = tangent_arc(+1, BOW_IN)    # concave (+Y) edge
PT = (0.0, PIN_Z)
PB = (0.0, -PIN_Z)
tL_top = tpoint((aL, bL), RL, PT)
tL_bot = tpoint((aL, bL), RL, PB)
tR_top = tpoint((aR, bR), RR, PT)
tR_bot = tpoint((aR, bR), RR, PB)


def side_wire_wp(x0=0.0):
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .moveTo(*tR_top)
        .threePointArc((0.0, PIN_Z + R_TOP), tL_top)
        .threePointArc(arc_mid((aL, bL), RL, tL_top, tL_bot), tL_bot)
        .threePointArc((0.0, -PIN_Z - R_BOT), tR_bot)
        .threePointArc(arc_mid((aR, bR), RR, tR_bot, tR_top), tR_top)
        .close()
    )


XL = X_MIN - 10.0
XW = X_MAX - X_MIN + 20.0
side = side_wire_wp(XL).extrude(XW)

# ---------------- front (X-Z) profile with joggles ----------------
ZT = PIN_Z + R_TOP + 10.0
ZB = -PIN_Z - R_BOT - 10.0

front = (
    cq.Workplane("XZ")
    .moveTo(X_MIN, ZT)
    .lineTo(X_MIN, JOG_TOP[0])
    .spline([(X_BODY, JOG_TOP[1])], tangents=[(0, -1), (0, -1)], includeCurrent=True)
    .lineTo(X_BODY, ZB)
    .lineTo(X_MAX, ZB)
    .lineTo(X_MAX, ZT)
    .close()
    .extrude(BIG, both=True)
)

# lower -X tine extension: S-shaped joggle, swept along Y on a slant so the
# joggle stays square to the (leaning) lower arm
Y0 = -BIG / 2.0
ext_face = (
    cq.Workplane("XZ", origin=(0, Y0, JOG_BOT_SKEW * (Y0 - JOG_BOT_YREF)))
    .moveTo(X_BODY + 4.0, JOG_BOT[0])
    .lineTo(X_BODY, JOG_BOT[0])
    .spline([(X_MIN, JOG_BOT[1])], tangents=[(0, -1), (0, -1)], includeCurrent=True)
    .lineTo(X_MIN, ZB - 10.0)
    .lineTo(X_BODY + 4.0, ZB - 10.0)
    .close()
    ._getFaces()[0]
)
ext = cq.Solid.extrudeLinear(ext_face, cq.Vector(0, BIG, BIG * JOG_BOT_SKEW))
front = front.union(cq.Workplane("XY").add(ext)).clean()

body = side.intersect(front)

# ---------------- clevis slots (through in Y, square to the arm) ----------
def slot_tool(gap, z_face, tilt, y_front, up):
    """Prism with an X-Z rectangular section swept along (0, 1, tilt), so the
    slot floor/roof is the plane z = z_face + tilt * (y - y_front)."""
    z0 = z_face + tilt * (Y0 - y_front)
    z_far = ZT + 30.0 if up else ZB - 30.0
    face = (
        cq.Workplane("XZ", origin=(0, Y0, 0))
        .polyline([(gap[0], z0), (gap[1], z0), (gap[1], z_far), (gap[0], z_far)])
        .close()
        ._getFaces()[0]
    )
    return cq.Workplane("XY").add(
        cq.Solid.extrudeLinear(face, cq.Vector(0, BIG, BIG * tilt))
    )


body = body.cut(slot_tool(TOP_GAP, TOP_SLOT_Z, TOP_SLOT_TILT, SLOT_Y_FRONT_T, True))
body = body.cut(slot_tool(BOT_GAP, BOT_SLOT_Z, BOT_SLOT_TILT, SLOT_Y_FRONT_B, False))


# ---------------- windows (through X) ----------------
def window(w):
    z_in, z_out, y0, m = w["z_in"], w["z_out"], w["y_ref"], w["slope"]
    ya, yb = -45.0, 25.0
    za = z_out + m * (ya - y0)
    zb = z_out + m * (yb - y0)
    band = (
        cq.Workplane("YZ", origin=(XL, 0, 0))
        .polyline([(ya, z_in), (yb, z_in), (yb, zb), (ya, za)])
        .close()
        .extrude(XW)
    )
    inner = side_wire_wp(XL).offset2D(-WIN_MARGIN).extrude(XW)
    wv = band.intersect(inner)
    return wv.edges("|X").fillet(WIN_R)


body = body.cut(window(WIN1)).cut(window(WIN2))

# ---------------- conical pad on the top +X tine inner face ----------------
pad = cq.Workplane("XY").add(
    cq.Solid.makeCone(PAD_R_BASE, PAD_R, TOP_GAP[1] - PAD_X,
                      cq.Vector(TOP_GAP[1], 0, PIN_Z), cq.Vector(-1, 0, 0))
)
pad = pad.intersect(side_wire_wp(PAD_X - 1.0).extrude(TOP_GAP[1] - PAD_X + 2.0))
body = body.union(pad).clean()

# ---------------- edge rounds (one fillet pass, per-edge radii) ----------
def edge_radius(e):
    pts = [v.toTuple() for v in e.Vertices()] + [e.positionAt(0.5).toTuple()]
    xs = [p[0] for p in pts]
    for z, tilt, yf, gap, rc, re in (
        (TOP_SLOT_Z, TOP_SLOT_TILT, SLOT_Y_FRONT_T, TOP_GAP, TOP_SLOT_R, TOP_SLOT_EDGE_R),
        (BOT_SLOT_Z, BOT_SLOT_TILT, SLOT_Y_FRONT_B, BOT_GAP, BOT_SLOT_R, BOT_SLOT_EDGE_R),
    ):
        if all(abs(p[2] - z - tilt * (p[1] - yf)) < 1e-3 for p in pts):
            if max(xs) - min(xs) > 1.0:
                # floor/roof meets front (-Y) or back (+Y) face
                return re[0] if pts[-1][1] < 0 else re[1]
            if all(abs(x - gap[0]) < 1e-3 for x in xs):
                return rc[0]                # inner corner of the slot (-X)
            if all(abs(x - gap[1]) < 1e-3 for x in xs):
                return rc[1]                # inner corner of the slot (+X)
    return EDGE_R


def fillet_all(wp):
    from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
    solid = wp.val()
    mk = BRepFilletAPI_MakeFillet(solid.wrapped)
    for e in solid.Edges():
        mk.Add(edge_radius(e), e.wrapped)
    mk.Build()
    if not mk.IsDone():
        return wp                           # fall back to sharp edges
    out = cq.Shape.cast(mk.Shape())
    return cq.Workplane("XY").add(out) if out.isValid() else wp


body = fillet_all(body)

# ---------------- keyhole pocket (outer face of bottom -X tine) ----------
kz0 = -PIN_Z + KEY_CIRC[1]
kz1 = -PIN_Z + KEY_SLOT[2]
kc = (
    cq.Workplane("YZ", origin=(X_MIN - 1.0, 0, 0))
    .center(KEY_CIRC[0], kz0)
    .circle(KEY_CIRC[2])
    .extrude(KEY_DEPTH + 1.0)
)
ks = (
    cq.Workplane("YZ", origin=(X_MIN - 1.0, 0, 0))
    .center(KEY_SLOT[0], 0.5 * (kz0 + kz1))
    .slot2D(kz1 - kz0 + KEY_SLOT[1], KEY_SLOT[1], 90)
    .extrude(KEY_DEPTH + 1.0)
)
body = body.cut(kc.union(ks))

# ---------------- pin holes ----------------
for zp in (PIN_Z, -PIN_Z):
    hole = (
        cq.Workplane("YZ", origin=(XL, 0, 0))
        .center(0.0, zp)
        .circle(PIN_D / 2.0)
        .extrude(XW)
    )
    body = body.cut(hole)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
